"""Branching strut lattice filling a cube, grown outward from a central spine.

Layout (Z up):
* a thin (knurled, modelled plain) spine rod runs along the Y axis through the
  whole cube, with a small cube block sitting on it at the middle;
* square-section struts leave the spine at a few stations and branch outward
  in Y-forks and gently kinked runs until they reach the cube faces, where
  they turn and run along the faces (dense skin on all six faces);
* the lattice has two-fold rotational symmetry about the spine (Y axis):
  one half is grown, the other half is the same half turned 180 deg;
* one forked strut pokes out of the top face and its rotated twin pokes out
  of the bottom face; a branch tip reaches into two opposite cube corners.

The branching is grown with a space-colonisation rule toward a fixed set of
target points; the points come from a fixed-seed integer stream (splitmix64),
so the script is fully deterministic.  Every run of struts is one mitred
square-section solid; all runs are fused with the spine into one solid.
"""
import math
import numpy as np
import cadquery as cq

# ---------------------------------------------------------------- parameters
CUBE = 90.0             # size of the lattice cube (outer faces of skin struts)
STRUT = 1.6             # square strut section (mm)
SPINE = 1.6             # diameter of the central (knurled) spine rod (mm)
HUB = 3.2               # cube block on the spine (mm)
STEP = 12.0             # mean strut segment length (mm)
STEP_VAR = 0.4          # +- fraction of segment length variation
MOMENTUM = 0.5          # how strongly a run keeps its direction
JITTER = 0.3            # random kink added to every growth step
N_INNER = 300           # growth target points inside the cube
N_FACE = 1200           # growth target points on the cube faces
FACE_T = 1.0            # depth of the face target layer (mm)
SPINE_CLEAR = 10.0      # no targets this close to the spine axis (mm)
INFLUENCE = 35.0        # reach of a target point (mm)
KILL = 11.0             # target is consumed when a node gets this close (mm)
MIN_SEP = 6.5           # minimum distance between lattice nodes (mm)
MAX_CHILD = 3           # at most a three-way split at a node
MAX_TURN = 120.0        # sharper kinks start a new run instead of a mitre (deg)
MAX_NODES = 400         # node budget for the grown half
ITERS = 60
ROOT_Y = [-29.0, -10.0, 0.0, 16.0, 27.0]   # spine stations the branches leave from
SPOKE_ANG = [[22.0, -62.0], [0.0, -72.0], [80.0, -16.0], [0.0, -27.0], [44.0]]  # spoke angles per station (deg from +X about Y)
SPOKE_SEG = 3           # segments in each spoke
SPOKE_DY = 1.0          # axial tilt range of a spoke
SPOKE_JIT = 0.12        # kink of the spoke segments
SEED = 1

# fork poking out of the bottom face (its 180-deg twin pokes out of the top)
SPUR = [(18.7, 10.4, -43.0), (18.7, 20.0, -48.9), (23.9, 27.8, -44.5)]
# branch tips reaching into the (+X,-Y,-Z) cube corner (and its twin corner)
TIPS = [(43.0, -43.5, -44.2)]

H = CUBE / 2.0
LIM = H - STRUT / 2.0   # centre-line limit so skin struts end flush at H


# ------------------------------------------------------- deterministic stream
class Stream:
    """splitmix64 integer stream -> floats in [0, 1)."""

    def __init__(self, seed):
        self.s = seed & 0xFFFFFFFFFFFFFFFF

    def rand(self):
        self.s = (self.s + 0x9E3779B97F4A7C15) & 0xFFFFFFFFFFFFFFFF
        z = self.s
        z = ((z ^ (z >> 30)) * 0xBF58476D1CE4E5B9) & 0xFFFFFFFFFFFFFFFF
        z = ((z ^ (z >> 27)) * 0x94D049BB133111EB) & 0xFFFFFFFFFFFFFFFF
        z = z ^ (z >> 31)
        return (z >> 11) / float(1 << 53)


# ----------------------------------------------------------- grow the lattice
def targets(rs):
    """Growth targets through the whole cube: a sparse interior cloud plus a
    dense layer just under the faces."""
    pts = []
    for _ in range(N_INNER):
        pts.append([(2 * rs.rand() - 1) * LIM for _ in range(3)])
    for _ in range(N_FACE):
        p = [(2 * rs.rand() - 1) * LIM for _ in range(3)]
        ax = min(int(rs.rand() * 3), 2)
        p[ax] = (1 if rs.rand() < 0.5 else -1) * (LIM - FACE_T * rs.rand())
        pts.append(p)
    A = np.array(pts)
    return A[np.hypot(A[:, 0], A[:, 2]) > SPINE_CLEAR]


def turned(a):
    """180 deg turn about the Y axis (the lattice's symmetry)."""
    b = np.array(a, float)
    b[..., 0] *= -1.0
    b[..., 2] *= -1.0
    return b


def spokes(rs):
    """Stations on the spine and the straight spokes leaving them."""
    nodes = [[0.0, y, 0.0] for y in ROOT_Y]
    parent = [-1] * len(ROOT_Y)
    for ri, y in enumerate(ROOT_Y):
        for th in [math.radians(a) for a in SPOKE_ANG[ri]]:
            dy = (rs.rand() - 0.5) * SPOKE_DY * abs(math.sin(th))   # flat spokes stay flat
            dv0 = np.array([math.cos(th), dy, math.sin(th)])
            dv0 /= np.linalg.norm(dv0)
            cur, pos = ri, np.array([0.0, y, 0.0])
            for _ in range(SPOKE_SEG):
                dv = dv0 + np.array([rs.rand() - 0.5 for _ in range(3)]) * SPOKE_JIT
                dv /= np.linalg.norm(dv)
                pos = np.clip(pos + dv * STEP * (1 + STEP_VAR * (2 * rs.rand() - 1)), -LIM, LIM)
                nodes.append(list(pos))
                parent.append(cur)
                cur = len(nodes) - 1
    return np.array(nodes, float), parent


def colonize():
    """Space colonisation of one half; the other half is its 180 deg turn about
    Y, and both halves compete for the same targets."""
    rs = Stream(SEED)
    A = targets(rs)
    nodes, parent = spokes(rs)
    alive = np.ones(len(A), bool)
    for _ in range(ITERS):
        idx = np.where(alive)[0]
        if len(idx) == 0:
            break
        Aa = A[idx]
        both = np.vstack([nodes, turned(nodes)])
        d = np.linalg.norm(Aa[:, None, :] - both[None, :, :], axis=2)
        kill = d.min(axis=1) < KILL
        alive[idx[kill]] = False
        Aa, d = Aa[~kill], d[~kill]
        if len(Aa) == 0:
            break
        nn = d.argmin(axis=1)
        ok = d[np.arange(len(Aa)), nn] < INFLUENCE
        if not ok.any():
            break
        pull = {}
        for a, n in zip(Aa[ok], nn[ok]):
            if n >= len(nodes):          # nearest is in the turned half
                n, a = n - len(nodes), turned(a)
            v = a - nodes[n]
            pull.setdefault(int(n), []).append(v / np.linalg.norm(v))
        nchild = np.zeros(len(nodes), int)
        for p in parent:
            if p >= 0:
                nchild[p] += 1
        new, newp = [], []
        for n in sorted(pull):
            if nchild[n] >= MAX_CHILD or parent[n] < 0:
                continue        # only the spokes leave the spine
            if np.sum(np.abs(nodes[n]) > LIM - 1e-6) >= 2:
                continue        # a run that reached a cube edge stops there
            v = np.sum(pull[n], axis=0)
            if np.linalg.norm(v) < 1e-6:
                continue
            v = v / np.linalg.norm(v)
            pd = nodes[n] - nodes[parent[n]]
            v = v + MOMENTUM * pd / np.linalg.norm(pd)
            v = v / np.linalg.norm(v)
            v = v + np.array([rs.rand() - 0.5 for _ in range(3)]) * JITTER
            v = v / np.linalg.norm(v)
            q = np.clip(nodes[n] + v * STEP * (1 + STEP_VAR * (2 * rs.rand() - 1)), -LIM, LIM)
            near = [both] + ([np.array(new), turned(np.array(new))] if new else [])
            near = np.vstack(near + [turned(q)[None, :]])
            if np.min(np.linalg.norm(near - q, axis=1)) < MIN_SEP:
                continue
            new.append(q)
            newp.append(n)
        if not new:
            break
        nodes = np.vstack([nodes, new])
        parent += newp
        if len(nodes) > MAX_NODES:
            break
    return nodes, parent


def tree_runs(nodes, parent):
    """Split the tree into runs; at a fork the best-aligned child continues."""
    children = [[] for _ in nodes]
    for i, p in enumerate(parent):
        if p >= 0:
            children[p].append(i)
    stack = [[i, c] for i in range(len(nodes)) if parent[i] < 0 for c in children[i]]
    runs = []
    while stack:
        ch = stack.pop()
        while children[ch[-1]]:
            last = ch[-1]
            dp = nodes[last] - nodes[ch[-2]]
            dp = dp / np.linalg.norm(dp)

            def align(c):
                v = nodes[c] - nodes[last]
                return float(np.dot(v / np.linalg.norm(v), dp))

            kids = children[last]
            best = max(kids, key=align)
            stack.extend([[last, c] for c in kids if c != best])
            if align(best) < math.cos(math.radians(MAX_TURN)):
                stack.append([last, best])      # too sharp for a mitre: new run
                break
            ch.append(best)
        pts = [nodes[i].copy() for i in ch]
        if parent[ch[0]] < 0:
            # a spoke: continue it through the spine into its turned twin so
            # the pair is one run crossing the spine (no coincident end caps)
            pts = list(turned(pts[:0:-1])) + pts
        else:
            # side run of a fork: start it inside the parent strut to close the crotch
            d0 = pts[1] - pts[0]
            p0 = pts[0] - d0 / np.linalg.norm(d0) * (STRUT / 2.0)
            if np.all(np.abs(p0) <= LIM):
                pts[0] = p0
        runs.append((pts, parent[ch[0]] < 0))
    return runs


# ------------------------------------------------------------ strut geometry
def rot_to(a, b):
    v = np.cross(a, b)
    s = np.linalg.norm(v)
    if s < 1e-12:
        return np.eye(3)
    k = v / s
    K = np.array([[0, -k[2], k[1]], [k[2], 0, -k[0]], [-k[1], k[0], 0]])
    ang = math.atan2(s, float(np.dot(a, b)))
    return np.eye(3) + math.sin(ang) * K + (1 - math.cos(ang)) * K @ K


def run_solid(P, w):
    """Mitred square-section bar along the polyline P, flat square ends."""
    P = [np.asarray(p, float) for p in P]
    n = len(P) - 1
    d = [(P[i + 1] - P[i]) / np.linalg.norm(P[i + 1] - P[i]) for i in range(n)]
    ref = np.array([0, 0, 1.0]) if abs(d[0][2]) < 0.9 else np.array([1.0, 0, 0])
    u = np.cross(ref, d[0])
    u /= np.linalg.norm(u)
    h = w / 2.0
    frames = []
    for i in range(n):
        if i:
            u = rot_to(d[i - 1], d[i]) @ u
            u = u - np.dot(u, d[i]) * d[i]
            u /= np.linalg.norm(u)
        v = np.cross(d[i], u)
        frames.append([sx * h * u + sy * h * v for sx, sy in ((-1, -1), (1, -1), (1, 1), (-1, 1))])
    secs = [[P[0] + c for c in frames[0]]]
    for i in range(1, n):
        m = d[i - 1] + d[i]
        m /= np.linalg.norm(m)
        secs.append([P[i] + c - np.dot(c, m) / np.dot(d[i - 1], m) * d[i - 1] for c in frames[i - 1]])
    secs.append([P[n] + c for c in frames[n - 1]])

    def poly(pts):
        return cq.Face.makeFromWires(
            cq.Wire.makePolygon([cq.Vector(*map(float, p)) for p in pts], close=True))

    faces = [poly(secs[0][::-1]), poly(secs[-1])]
    for a, b in zip(secs[:-1], secs[1:]):
        for k in range(4):
            k2 = (k + 1) % 4
            faces.append(poly([a[k], a[k2], b[k2], b[k]]))
    return cq.Solid.makeSolid(cq.Shell.makeShell(faces))


def fuse_all(parts):
    """Boolean union of all parts, checked against the summed volume (the
    overlaps at joints only remove a few percent); falls back to batch-wise
    fusing if a single multi-argument fuse goes wrong."""
    total = sum(p.Volume() for p in parts)

    def good(shape):
        return shape.isValid() and shape.Volume() > 0.85 * total

    out = parts[0].fuse(*parts[1:]).clean()
    if good(out):
        return out
    merged = []
    for i in range(0, len(parts), 25):
        b = parts[i:i + 25]
        merged.append(b[0].fuse(*b[1:]).clean() if len(b) > 1 else b[0])
    out = merged[0]
    for m in merged[1:]:
        out = out.fuse(m).clean()
    if good(out):
        return out
    return cq.Compound.makeCompound(parts)


# ------------------------------------------------------------------ assemble
nodes, parent = colonize()


def nearest(p):
    return nodes[np.argmin(np.linalg.norm(nodes - p, axis=1))]


half = tree_runs(nodes, parent)
spur = [np.array(p, float) for p in SPUR]
half.append(([nearest(spur[0])] + spur, False))   # spur grows out of the nearest node
for t in TIPS:
    t = np.array(t, float)
    half.append(([nearest(t), t], False))
# spoke runs already hold both halves; every other run gets its turned twin
runs = [r for r, _ in half] + [list(turned(r)) for r, whole in half if not whole]

solids = [run_solid(r, STRUT) for r in runs]
# central spine rod along Y and the cube block sitting on it
solids.append(cq.Solid.makeCylinder(SPINE / 2.0, CUBE, pnt=cq.Vector(0, -H, 0), dir=cq.Vector(0, 1, 0)))
solids.append(cq.Solid.makeBox(HUB, HUB, HUB, pnt=cq.Vector(-HUB / 2, -HUB / 2, SPINE / 2 - 0.05)))

lattice = fuse_all(solids)
result = cq.Workplane("XY").newObject(lattice.Solids())

VIEW = {"azimuth": 45, "elevation": 26}
